import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Flat lever / handle lying in the XZ plane, thickness along Y.
# Pivot end (hole) at the origin, grip end down and to the right.
ARM_W = 20.0             # width of the straight arm (= pivot end diameter)
R_HOLE_END = ARM_W / 2   # radius of the rounded pivot end
ARM_LEN = 124.6          # centre distance pivot -> grip end
ARM_ANG = -47.9          # direction of the arm in the XZ plane (deg from +X)
R_GRIP_END = 10.0        # radius of the rounded grip end
GRIP_FLARE = 15.3        # lower grip edge is this much steeper than the arm (deg)
NOTCH_S = 75.5           # where the lower arm edge leaves its straight line
R_NOTCH_CVX = 7.1        # convex arc of the S-shaped finger notch
R_NOTCH_CCV = 7.1        # concave arc of the S-shaped finger notch

T = 5.9                  # plate thickness (Y)
EDGE_R_BACK = 1.5        # perimeter edge rounding, back face (+Y)
EDGE_R_FRONT = 1.2       # perimeter edge rounding, front face (-Y)

BOSS_D = 15.0            # round boss on the back face (+Y)
BOSS_H = 1.8
BOSS_TOP_R = 0.9         # convex rounding of the boss top
BOSS_BASE_R = 0.9        # concave flare into the back face

CBORE_D = 10.4           # counterbore from the front face (-Y)
CBORE_DEPTH = T          # runs through the plate; the boss carries the floor
HOLE_D = 3.3             # small through hole
HOLE_CHAMFER = 0.4       # soft entry of the small hole on the boss


# ---------------- 2D helpers (x = X, y = Z) ----------------
def add(p, q):
    return (p[0] + q[0], p[1] + q[1])


def sub(p, q):
    return (p[0] - q[0], p[1] - q[1])


def mul(p, s):
    return (p[0] * s, p[1] * s)


def dot(p, q):
    return p[0] * q[0] + p[1] * q[1]


def unit(p):
    l = math.hypot(p[0], p[1])
    return (p[0] / l, p[1] / l)


def dirn(deg):
    r = math.radians(deg)
    return (math.cos(r), math.sin(r))


def arc_mid(c, r, p, q):
    """mid point of the (short) arc of radius r about c between p and q."""
    return add(c, mul(unit(add(sub(p, c), sub(q, c))), r))


# ---------------- outline ----------------
C1 = (0.0, 0.0)
a = dirn(ARM_ANG)                    # along the arm
n = (-a[1], a[0])                    # normal towards the upper (straight) edge
C2 = add(C1, mul(a, ARM_LEN))

# straight upper edge, tangent to both end circles
TU1 = add(C1, mul(n, R_HOLE_END))
TU2 = add(C2, mul(n, R_GRIP_END))

# lower grip edge, tangent to the grip end circle
g = dirn(ARM_ANG - GRIP_FLARE)
ng = (g[1], -g[0])                   # outward normal of the grip edge
TG = add(C2, mul(ng, R_GRIP_END))

# lower arm edge
TL1 = sub(C1, mul(n, R_HOLE_END))

# S-shaped notch: convex arc tangent to the arm edge, concave arc tangent
# to the grip edge, both arcs tangent to each other
T_L = add(TL1, mul(a, NOTCH_S))
Ca = add(T_L, mul(n, R_NOTCH_CVX))
Q = add(TG, mul(ng, R_NOTCH_CCV))
w = sub(Ca, Q)
rr = R_NOTCH_CVX + R_NOTCH_CCV
wg = dot(w, g)
u = wg + math.sqrt(wg * wg - dot(w, w) + rr * rr)
Cb = add(Q, mul(g, u))
T_ab = add(Ca, mul(sub(Cb, Ca), R_NOTCH_CVX / rr))
T_G = sub(Cb, mul(ng, R_NOTCH_CCV))
m_ccv = arc_mid(Cb, R_NOTCH_CCV, T_G, T_ab)
m_cvx = arc_mid(Ca, R_NOTCH_CVX, T_ab, T_L)

# rounded ends
m_back = sub(C1, mul(a, R_HOLE_END))
ang_n = math.atan2(n[1], n[0])
ang_g = math.atan2(ng[1], ng[0])
sweep = (ang_n - ang_g) % (2 * math.pi)        # clockwise from n to ng
m_grip = add(C2, mul(dirn(math.degrees(ang_n - sweep / 2)), R_GRIP_END))

plate = (
    cq.Workplane("XZ", origin=(0, T / 2, 0))
    .moveTo(*TU1)
    .lineTo(*TU2)
    .threePointArc(m_grip, TG)
    .lineTo(*T_G)
    .threePointArc(m_ccv, T_ab)
    .threePointArc(m_cvx, T_L)
    .lineTo(*TL1)
    .threePointArc(m_back, TU1)
    .close()
    .extrude(T)                      # Y from +T/2 (back) to -T/2 (front)
)
plate = plate.faces(">Y").edges().fillet(EDGE_R_BACK)
plate = plate.faces("<Y").edges().fillet(EDGE_R_FRONT)

# ---------------- boss on the back face (+Y) ----------------
# revolved profile: concave base fillet + convex top fillet
rb, fb, ft = BOSS_D / 2, BOSS_BASE_R, BOSS_TOP_R
y0 = T / 2
k = math.sqrt(0.5)
bp = (
    cq.Workplane("XY")
    .moveTo(0, y0 - 0.3)
    .lineTo(rb + fb, y0 - 0.3)
    .lineTo(rb + fb, y0)
    .threePointArc((rb + fb - fb * k, y0 + fb - fb * k), (rb, y0 + fb))
)
if BOSS_H - ft - fb > 1e-3:
    bp = bp.lineTo(rb, y0 + BOSS_H - ft)
boss = (
    bp.threePointArc((rb - ft + ft * k, y0 + BOSS_H - ft + ft * k),
                     (rb - ft, y0 + BOSS_H))
    .lineTo(0, y0 + BOSS_H)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = plate.union(boss)

# ---------------- counterbore (front) and small through hole ----------------
yb = y0 + BOSS_H                      # back face of the boss
hole_tool = (
    cq.Workplane("XY")
    .moveTo(0, -T / 2 - 1.0)
    .lineTo(CBORE_D / 2, -T / 2 - 1.0)
    .lineTo(CBORE_D / 2, -T / 2 + CBORE_DEPTH)
    .lineTo(HOLE_D / 2, -T / 2 + CBORE_DEPTH)
    .lineTo(HOLE_D / 2, yb - HOLE_CHAMFER)
    .lineTo(HOLE_D / 2 + HOLE_CHAMFER, yb)
    .lineTo(HOLE_D / 2 + HOLE_CHAMFER, yb + 1.0)
    .lineTo(0, yb + 1.0)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.cut(hole_tool)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
